"""Egg-shaped dome cover with three counterbored screw holes and three
tubular bosses under a shallow rectangular relief on the flat underside.

The dome is half of a smooth body of revolution about the Y axis (circular
cross sections): narrow rounded tip at -Y, blunt wide end at +Y, widest
station about 63 % of the length from the narrow tip.
"""
import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
LENGTH = 100.0        # overall length along Y (narrow tip at -Y, wide end at +Y)
R_MAX = 32.0          # max half-width == max height (circular cross sections)
AXIS_DROP = 0.52      # revolve axis sits this far below the flat base
SEAM_ANGLE = 0.0      # where the (cut away) revolve seam sits, below the base

# profile stations: (distance from the narrow tip, radius) as fractions of
# LENGTH and R_MAX; the end tangents are normal to the axis (smooth tips)
PROFILE = [
    (0.03, 0.2500), (0.08, 0.4000), (0.15, 0.5594), (0.25, 0.7438),
    (0.37, 0.8938), (0.50, 0.9781), (0.63, 1.0000), (0.75, 0.9656),
    (0.85, 0.8281), (0.94, 0.5625), (0.98, 0.3250),
]

# screw bosses / holes  (x, y) on the base plane
HOLES = [(0.0, 32.0), (-11.2, 12.5), (11.2, 12.5)]
BOSS_D = 8.0
BOSS_H = 6.5          # boss end below the main flat base
BOSS_CHAMFER = 0.4
THRU_D = 5.0          # through hole in boss and dome
CBORE_D = 10.0        # counterbore from the top of the dome
CBORE_FLOOR_Z = 6.0   # counterbore floor height above the base

# shallow rectangular relief in the underside (holds the bosses)
REC_HALF_W = 23.0
REC_Y0 = -11.3        # front edge of the relief; it runs out at the wide end
REC_DEPTH = 0.75

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- dome: revolve a spline profile ----------------
y_tip = -LENGTH / 2
y_wide = LENGTH / 2
spl_pts = (
    [(0.0, y_tip)]
    + [(f_r * R_MAX, y_tip + f_d * LENGTH) for (f_d, f_r) in PROFILE]
    + [(0.0, y_wide)]
)
# chord-length parameters + unit end tangents keep the spline fair
spl_par = [0.0]
for (xa, ya), (xb, yb) in zip(spl_pts[:-1], spl_pts[1:]):
    spl_par.append(spl_par[-1] + math.hypot(xb - xa, yb - ya))

profile = (
    cq.Workplane("XY")
    .moveTo(0.0, y_tip)
    .spline(
        spl_pts[1:],
        tangents=[(1.0, 0.0), (-1.0, 0.0)],
        parameters=spl_par,
        scale=False,
        includeCurrent=True,
    )
    .close()
)

# full solid of revolution, axis a hair below the base plane (keeps the
# narrow-tip pole off the flat bottom), then keep everything above z = 0
body = (
    profile.revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 1, 0), SEAM_ANGLE)   # revolve seam stays under the base
    .translate((0, 0, -AXIS_DROP))
    .intersect(
        cq.Workplane("XY").box(
            4 * R_MAX, 2 * LENGTH, 2 * R_MAX, centered=(True, True, False)
        )
    )
)

# stretch vertically so the crown is back at R_MAX (cross sections stay
# practically semicircular); the dome ends up as a single NURBS face
z_stretch = R_MAX / (R_MAX - AXIS_DROP)
stretch = cq.Matrix(
    [[1.0, 0.0, 0.0, 0.0], [0.0, 1.0, 0.0, 0.0], [0.0, 0.0, z_stretch, 0.0]]
)
body = cq.Workplane("XY").add(body.val().transformGeometry(stretch))

# ---------------- underside relief ----------------
relief = (
    cq.Workplane("XY")
    .box(2 * REC_HALF_W, LENGTH, REC_DEPTH, centered=(True, False, False))
    .translate((0, REC_Y0, 0))
)
body = body.cut(relief)

# ---------------- bosses ----------------
for (x, y) in HOLES:
    boss = (
        cq.Workplane("XY")
        .workplane(offset=-BOSS_H)
        .circle(BOSS_D / 2)
        .extrude(BOSS_H + REC_DEPTH)
        .faces("<Z")
        .edges()
        .chamfer(BOSS_CHAMFER)
        .rotate((0, 0, 0), (0, 0, 1), 135)   # park the cylinder seam at the back
        .translate((x, y, 0))
    )
    body = body.union(boss)

# ---------------- counterbored through holes ----------------
for (x, y) in HOLES:
    thru = (
        cq.Workplane("XY")
        .workplane(offset=-BOSS_H - 1)
        .center(x, y)
        .circle(THRU_D / 2)
        .extrude(R_MAX + BOSS_H + 5)
    )
    cbore = (
        cq.Workplane("XY")
        .workplane(offset=CBORE_FLOOR_Z)
        .center(x, y)
        .circle(CBORE_D / 2)
        .extrude(R_MAX + 5)
    )
    body = body.cut(thru).cut(cbore)

result = body
